import math
import cadquery as cq

# ---------------------------------------------------------------------------
# 90 deg mitred pipe elbow (closed ends) with an inspection cap on the outer
# corner.  Origin = intersection of the two leg axes.
#   horizontal leg : axis along X, end face towards -X
#   vertical leg   : axis along Z, end face towards -Z
#   the inner corner is bridged by a ruled transition between the legs,
#   the outer corner (x + z > C_SEAM) is replaced by a ruled "dome" that
#   narrows to a round inspection cap (seat ring, lid with a shallow dome,
#   pry notch, two bumps, embossed mark) facing +X, tilted CAP_TILT deg up.
# ---------------------------------------------------------------------------
R = 40.5            # pipe outer radius
LH = 55.7           # horizontal leg: corner -> end face
LV = 47.3           # vertical leg: corner -> end face
C_SEAM = 11.2       # seam plane  x + z = C_SEAM
CAP_TILT = 17.5     # cap plane tilt: its normal is this many deg above +X
CAP_CX = 35.4       # centre of the dome end circle (cap seat)
CAP_CZ = 10.15
SEAT_R = 31.0       # dome end radius
RIM_H = 0.9         # conical seat ring: rises this much along the cap axis ...
RIM_R = 29.3        # ... while narrowing to this radius
LID_R = 28.9        # lid radius
LID_WALL = 0.7      # lid side wall above the seat ring
LID_DOME = 2.4      # shallow spherical lid rises this much above its rim
NOTCH_W = 6.0       # pry notch (V) at the top of the cap
NOTCH_IN = 1.6      # notch apex this far inside the lid edge
BUMP_R = 2.5        # two small bumps at the lower lid edge
BUMP_PR = 27.4      # bump pitch radius
BUMP_ANG = 124.0    # bump angle from the lid "up" direction (+/-)
BUMP_SINK = 1.3     # bump centres sit this far below the lid rim
LOGO_X, LOGO_Y = 0.0, 0.0    # logo offset on the lid (local: x=+Y, y=up)
LOGO_H = 0.25       # logo relief
END_CH = 0.6        # chamfer at the closed bottom end
END_CH_H = 1.2      # chamfer at the closed horizontal end
SPIG_H = 4.8        # horizontal end: reduced band length
SPIG_IN = 0.3       # ... radial inset
VSTEP_H = 1.1       # vertical end: step height
VSTEP_IN = 2.2      # ... radial inset
BEND_R = 44.0       # inner swept bend: centre-line radius
PAD_X = -16.5       # little oval pad on top of the dome
PAD_L, PAD_W, PAD_TOP = 6.5, 4.5, 40.65   # pad top height (z)

BIG = 400.0
S2 = math.sqrt(2.0)


def _perp(n):
    a = cq.Vector(0, 1, 0) if abs(n.y) < 0.9 else cq.Vector(1, 0, 0)
    return a.cross(n).normalized()


def halfspace(point, normal):
    """Big box filling the side of plane(point, normal) opposite to normal."""
    n = cq.Vector(*normal).normalized()
    pl = cq.Plane(origin=cq.Vector(*point), xDir=_perp(n), normal=n)
    return cq.Workplane(pl).rect(BIG, BIG).extrude(-BIG).val()


def cyl(r, p0, d, length):
    return cq.Solid.makeCylinder(r, length, cq.Vector(*p0), cq.Vector(*d))


# ---------------- mitred elbow up to the seam plane -------------------------
# (cylinders turned so that their seam lines sit underneath / at the back)
cyl_h = cyl(R, (-LH, 0, 0), (1, 0, 0), LH + 2 * R).rotate(cq.Vector(0, 0, 0), cq.Vector(1, 0, 0), 180)
cyl_v = cyl(R, (0, 0, -LV), (0, 0, 1), LV + 2 * R).rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), 90)
seam_cut = halfspace((C_SEAM / 2, 0, C_SEAM / 2), (1, 0, 1))   # keep x+z <= c
leg_h = cyl_h.intersect(halfspace((0, 0, 0), (1, 0, -1))).intersect(seam_cut)
leg_v = cyl_v.intersect(halfspace((0, 0, 0), (-1, 0, 1))).intersect(seam_cut)
elbow = leg_h.fuse(leg_v).clean()

# ---------------- inner corner: ruled transition between the legs ---------
# the pipe section of the horizontal leg at x = -BEND_R is joined straight
# (ruled) to the section of the vertical leg at z = -BEND_R.
def _ring(pts):
    o, a, i, b = [cq.Vector(*p) for p in pts]
    return cq.Wire.assembleEdges([cq.Edge.makeThreePointArc(o, a, i), cq.Edge.makeThreePointArc(i, b, o)])


sec_h = _ring([(-BEND_R, 0, R), (-BEND_R, -R, 0), (-BEND_R, 0, -R), (-BEND_R, R, 0)])
sec_v = _ring([(R, 0, -BEND_R), (0, -R, -BEND_R), (-R, 0, -BEND_R), (0, R, -BEND_R)])
bend = cq.Solid.makeLoft([sec_h, sec_v], ruled=True)
elbow = elbow.fuse(bend.intersect(seam_cut)).clean()

# ---------------- seam wire (two elliptic arcs on the seam plane) ----------
t0 = math.degrees(math.acos(-C_SEAM / (2 * R)))
s0 = math.degrees(math.acos(C_SEAM / (2 * R)))
arc_h = cq.Edge.makeEllipse(R * S2, R, pnt=cq.Vector(C_SEAM, 0, 0), dir=cq.Vector(1, 0, 1),
                            xdir=cq.Vector(1, 0, -1), angle1=t0, angle2=360 - t0)
arc_v = cq.Edge.makeEllipse(R * S2, R, pnt=cq.Vector(0, 0, C_SEAM), dir=cq.Vector(1, 0, 1),
                            xdir=cq.Vector(1, 0, -1), angle1=-s0, angle2=s0)
seam_wire = cq.Wire.assembleEdges([arc_h, arc_v])

# ---------------- cap frame -------------------------------------------------
th = math.radians(CAP_TILT)
n_cap = cq.Vector(math.cos(th), 0, math.sin(th))
up_cap = cq.Vector(-math.sin(th), 0, math.cos(th))
ey = cq.Vector(0, 1, 0)
c_cap = cq.Vector(CAP_CX, 0, CAP_CZ)


def p_c(phi, r, off=0.0):
    """point near the cap plane: phi from the cap 'up' direction towards +Y"""
    f = math.radians(phi)
    return c_cap + n_cap * off + up_cap * (r * math.cos(f)) + ey * (r * math.sin(f))


cap_wire = cq.Wire.assembleEdges([
    cq.Edge.makeThreePointArc(p_c(90, SEAT_R), p_c(0, SEAT_R), p_c(-90, SEAT_R)),
    cq.Edge.makeThreePointArc(p_c(-90, SEAT_R), p_c(180, SEAT_R), p_c(90, SEAT_R)),
])
dome = cq.Solid.makeLoft([seam_wire, cap_wire], ruled=True)
body = elbow.fuse(dome).clean()

# ---------------- lid: conical seat ring, short lid wall, shallow dome -------
cap_plane = cq.Plane(origin=c_cap, xDir=ey, normal=n_cap)     # local y = up_cap
lid_top = RIM_H + LID_WALL                                     # lid rim height
lid_sph_r = (LID_R ** 2 + LID_DOME ** 2) / (2 * LID_DOME)
sph_c = c_cap + n_cap * (lid_top + LID_DOME - lid_sph_r)
rim = cq.Solid.makeCone(SEAT_R, RIM_R, RIM_H, pnt=c_cap, dir=n_cap)
lid = (cq.Workplane(cap_plane).workplane(offset=RIM_H - 0.01).circle(LID_R)
       .extrude(LID_WALL + LID_DOME + 1.0).val()
       .intersect(cq.Solid.makeSphere(lid_sph_r, pnt=sph_c, angleDegrees1=-90, angleDegrees2=90)))
body = body.fuse(rim).fuse(lid)

# two small bumps at the lower edge of the lid
for sgn in (1, -1):
    pb = p_c(sgn * BUMP_ANG, BUMP_PR, lid_top - BUMP_SINK)
    body = body.fuse(cq.Solid.makeSphere(BUMP_R, pnt=pb, angleDegrees1=-90, angleDegrees2=90))

# pry notch: V cut across the rim ring into the lid edge at the top
nw = NOTCH_W / 2
notch = (cq.Workplane(cap_plane)
         .polyline([(-nw, SEAT_R + 0.5), (nw, SEAT_R + 0.5), (0, LID_R - NOTCH_IN)]).close()
         .extrude(lid_top + LID_DOME + 1.0))
body = body.cut(notch.val())

# embossed logo on the lid (flag mark: pole + bar + box with a V cut-out)
lx, ly = LOGO_X, LOGO_Y
logo_pts = [(-8.0, 10.1), (-8.0, 18.2), (7.7, 18.2), (7.7, 11.2), (-0.4, 11.2),
            (-0.4, 16.6), (-6.6, 16.6), (-6.6, 10.1)]
logo = (cq.Workplane(cap_plane).workplane(offset=lid_top)
        .polyline([(lx + x, ly + y) for x, y in logo_pts]).close()
        .extrude(LID_DOME + 1.0).val())
tri = (cq.Workplane(cap_plane).workplane(offset=lid_top)
       .polyline([(lx + 0.7, ly + 15.9), (lx + 6.8, ly + 15.9), (lx + 4.8, ly + 12.6)]).close()
       .extrude(LID_DOME + 1.0).val())
logo = logo.cut(tri).intersect(cq.Solid.makeSphere(lid_sph_r + LOGO_H, pnt=sph_c,
                                                   angleDegrees1=-90, angleDegrees2=90))
body = body.fuse(logo)

# ---------------- closed ends: reduced bands with chamfered end edges --------
keep_h = (cq.Workplane("YZ").workplane(offset=-LH).circle(R - SPIG_IN).extrude(SPIG_H + 3)
          .faces("<X").edges().chamfer(END_CH_H).val())
band_h = cyl(R + 5, (-LH - 1, 0, 0), (1, 0, 0), SPIG_H + 1).cut(keep_h)
body = body.cut(band_h)
keep_v = (cq.Workplane("XY").workplane(offset=-LV).circle(R - VSTEP_IN).extrude(VSTEP_H + 3)
          .faces("<Z").edges().chamfer(END_CH).val())
band_v = cyl(R + 5, (0, 0, -LV - 1), (0, 0, 1), VSTEP_H + 1).cut(keep_v)
body = body.cut(band_v)

# ---------------- little oval pad on the top ---------------------------------
pad = (cq.Workplane("XY").workplane(offset=R - 2.0).center(PAD_X, 0)
       .ellipse(PAD_L / 2, PAD_W / 2).extrude(PAD_TOP - (R - 2.0)))
body = body.fuse(pad.val())

result = cq.Workplane("XY").add(body.clean())
